import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Tray plate: flat front face at Y=0, 3x3 pockets open toward +Y (back)
PLATE_W = 99.4           # square plate size (X and Z)
PLATE_T = 9.0            # plate thickness (Y)
PLATE_R = 18.0           # corner radius of the square outline

POCKET_PITCH = 30.35     # 3 x 3 grid pitch
POCKET_RIM_D = 27.8      # pocket (counterbore) diameter
POCKET_FLOOR_D = 18.5    # diameter of the shallow central recess
POCKET_DEPTH = 5.0       # counterbore depth (flat floor)
RECESS_DEPTH = 0.4       # shallow central recess in the pocket floor

RING_OD = 32.6           # raised broken ring around the centre pocket
RING_H = 0.9             # ring height above the back face
RING_GAP = 10.0          # width of the four gaps (cross-shaped cut)

# Loose discs (front faces flush with the plate front face)
DISC_D = 26.8
DISC_T = 6.0
DISC_EDGE_FILLET = 0.4
DISC_Z = 70.9            # disc centre height above plate centre
DISC1_X = -111.7         # disc with a central insert/boss
DISC2_X = -71.2          # disc with two small tabs near its bottom

BOSS_D = 10.2            # central insert of disc 1
BOSS_BACK = 1.5          # protrusion beyond back face
BOSS_FRONT = 0.7         # protrusion beyond front face

TAB_W = 1.2              # small thin tabs through the bottom of disc 2 (X width)
TAB_H = 0.25             # tab thickness (Z)
TAB_X = 3.3              # +/- offset from disc centre
TAB_Z = -12.4            # below disc centre
TAB_OUT = 1.1            # protrusion beyond each face

VIEW = {"azimuth": 45, "elevation": 26}


def xz_plane(y):
    """Workplane parallel to XZ with normal +Y at Y=y.
    Local x -> world +X, local y -> world -Z."""
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, 1, 0)))


# ---------------- plate ----------------
plate = (
    xz_plane(0)
    .rect(PLATE_W, PLATE_W)
    .extrude(PLATE_T)
    .edges("|Y")
    .fillet(PLATE_R)
)

# raised ring around the centre pocket, interrupted by a cross-shaped cut
ring = xz_plane(PLATE_T).circle(RING_OD / 2.0).extrude(RING_H)
cut_a = xz_plane(PLATE_T).rect(RING_GAP, RING_OD + 4).extrude(RING_H + 1)
cut_b = xz_plane(PLATE_T).rect(RING_OD + 4, RING_GAP).extrude(RING_H + 1)
ring = ring.cut(cut_a).cut(cut_b)
plate = plate.union(ring)

# pocket tool: revolved profile = counterbore with a flat floor and a shallow
# central recess (drawn in XY with x = radius, y = world Y, revolved about Y)
r_rim = POCKET_RIM_D / 2.0
r_floor = POCKET_FLOOR_D / 2.0
y_floor = PLATE_T - POCKET_DEPTH
y_top = PLATE_T + RING_H + 1.0
pocket_tool = (
    cq.Workplane("XY")
    .moveTo(0, y_floor - RECESS_DEPTH)
    .lineTo(r_floor, y_floor - RECESS_DEPTH)
    .lineTo(r_floor, y_floor)
    .lineTo(r_rim, y_floor)
    .lineTo(r_rim, y_top)
    .lineTo(0, y_top)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .val()
)
for i in (-1, 0, 1):
    for j in (-1, 0, 1):
        tool = pocket_tool.translate(cq.Vector(i * POCKET_PITCH, 0, j * POCKET_PITCH))
        plate = plate.cut(cq.Workplane("XY").add(tool))

# ---------------- disc 1 (with central boss/insert) ----------------
disc1 = xz_plane(0).center(DISC1_X, -DISC_Z).circle(DISC_D / 2.0).extrude(DISC_T)
disc1 = disc1.edges().fillet(DISC_EDGE_FILLET)
boss = (
    xz_plane(-BOSS_FRONT)
    .center(DISC1_X, -DISC_Z)
    .circle(BOSS_D / 2.0)
    .extrude(DISC_T + BOSS_FRONT + BOSS_BACK)
)
disc1 = disc1.union(boss)

# ---------------- disc 2 (with two small tabs at its bottom) ----------------
disc2 = xz_plane(0).center(DISC2_X, -DISC_Z).circle(DISC_D / 2.0).extrude(DISC_T)
disc2 = disc2.edges().fillet(DISC_EDGE_FILLET)
tab_z_local = -(DISC_Z + TAB_Z)
tabs = (
    xz_plane(-TAB_OUT)
    .pushPoints([(DISC2_X - TAB_X, tab_z_local), (DISC2_X + TAB_X, tab_z_local)])
    .rect(TAB_W, TAB_H)
    .extrude(DISC_T + 2 * TAB_OUT)
)
disc2 = disc2.union(tabs)

# three separate bodies: the tray plate and the two loose discs
result = cq.Workplane("XY").newObject(
    [cq.Compound.makeCompound([plate.val(), disc1.val(), disc2.val()])]
)
